import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 72.0            # overall body width (X)
H = 40.0            # body height (Z)
T_LUG = 11.0        # lug (ear) thickness
SLOT_W = W - 2 * T_LUG
EYE_A = 26.0        # eye nose semi-axis along Y (tip -> hole centre)
EYE_A_BACK = 22.0   # eye semi-axis along Y towards the plate
EYE_B = H / 2.0     # eye semi-axis along Z
EYE_EDGE_R = 3.0    # round on the eye outer rim
EYE_BULGE = 0.6     # eye outer faces are slightly domed ...
EYE_DOME_R = 330.0  # ... with this sphere radius
BODY_R = 7.5        # big rounds on the body / arm outer long edges
SIDE_ARC_R = 20.0   # -X side wall blends into the plate on this arc ...
SIDE_ARC_LEN = 12.0 # ... starting this far in front of the plate
SHOULDER_R = 3.0    # soften the sweep's edges
ARM_START_Y = 6.0   # where the square arm section starts (hole centre = 0)
SLOT_BOTTOM_Y = 41.4  # slot bottom, measured from hole centre (Y=0)
SLOT_RX = 7.0       # slot inner corner (elliptic) extent across the slot
SLOT_RY = 10.0      # ... and along the lug wall

PLATE_ANG = 22.4    # plate yaw (deg) about Z
PLATE_BACK_X = W / 2.0   # back/right corner of the plate is flush with +X face
PLATE_BACK_Y = 73.0      # ... at this Y
PLATE_T = 2.5
PLATE_H = 54.0
PLATE_LEN = 81.4

HOLE_Z = 1.2        # pin axis sits slightly above mid height
HOLE_D = 11.0
CB_D = 20.0         # counterbore on +X lug
CB_DEPTH = 7.0
HEX_AF = 18.0       # hex nut pocket on -X lug
HEX_DEPTH = 8.0

Y_MAX = 140.0       # raw body length before trimming by the plate plane

ang = math.radians(PLATE_ANG)
n = cq.Vector(math.sin(ang), math.cos(ang), 0)       # plate normal (away from lugs)
u = cq.Vector(-math.cos(ang), math.sin(ang), 0)      # along plate towards -X
p_back = cq.Vector(PLATE_BACK_X, PLATE_BACK_Y, 0)    # back face, +X end
p_front = p_back - n * PLATE_T                        # front face, +X end

# ---------------- main body (rounded box) ----------------
body = (
    cq.Workplane("XY")
    .box(W, Y_MAX - ARM_START_Y, H, centered=(True, False, True))
    .translate((0, ARM_START_Y, 0))
    .edges("|Y")
    .fillet(BODY_R)
)

# trim the body at the back face of the plate and round that end
big = 400.0
trimmer = cq.Workplane(cq.Plane(origin=p_back, xDir=u, normal=n)).rect(big, big).extrude(big)
body = body.cut(trimmer)

# the -X side wall sweeps inward on a large arc just before it meets the plate
y_front_left = (p_front.y + (p_front.x + W / 2.0) * math.tan(ang))  # plate front at X=-W/2
t_y = y_front_left - SIDE_ARC_LEN                                    # arc tangent point
arc_cx = -W / 2.0 + SIDE_ARC_R
corner_box = (
    cq.Workplane("XY", origin=(0, 0, -H))
    .center(-W / 2.0 - 10.0 + (SIDE_ARC_R + 10.0) / 2.0, t_y + 30.0)
    .rect(SIDE_ARC_R + 10.0, 60.0)
    .extrude(2 * H)
)
arc_disc = (
    cq.Workplane("XY", origin=(0, 0, -H))
    .center(arc_cx, t_y)
    .circle(SIDE_ARC_R)
    .extrude(2 * H)
)
body = body.cut(corner_box.cut(arc_disc))
# soften the edges where that sweep meets the top / bottom rounds
body = body.edges(
    cq.selectors.BoxSelector((-W / 2.0 - 1, t_y - 1, -H), (-W / 2.0 + SIDE_ARC_R, t_y + 40, H))
).fillet(SHOULDER_R)

# ---------------- clevis slot ----------------
y_front = -EYE_A - 10.0
slot = (
    cq.Workplane("XY", origin=(0, 0, -H))
    .moveTo(SLOT_W / 2.0, y_front)
    .lineTo(SLOT_W / 2.0, SLOT_BOTTOM_Y - SLOT_RY)
    .ellipseArc(SLOT_RX, SLOT_RY, 0, 90, startAtCurrent=True)
    .lineTo(-SLOT_W / 2.0 + SLOT_RX, SLOT_BOTTOM_Y)
    .ellipseArc(SLOT_RX, SLOT_RY, 90, 180, startAtCurrent=True)
    .lineTo(-SLOT_W / 2.0, y_front)
    .close()
    .extrude(2 * H)
)
body = body.cut(slot)


# ---------------- eyes (elliptic discs with small rim round) ----------------
def eye(outer_sign):
    x_in = outer_sign * (W / 2.0 - T_LUG)
    x_out = outer_sign * (W / 2.0 + EYE_BULGE)
    disc = (
        cq.Workplane("YZ", origin=(min(x_in, x_out), 0, 0))
        .moveTo(0, EYE_B)
        .ellipseArc(EYE_A, EYE_B, 90, 270, startAtCurrent=True)
        .ellipseArc(EYE_A_BACK, EYE_B, -90, 90, startAtCurrent=True)
        .close()
        .extrude(T_LUG + EYE_BULGE)
    )
    dome = cq.Workplane("XY").sphere(EYE_DOME_R).translate(
        (x_out - outer_sign * EYE_DOME_R, 0, HOLE_Z)
    )
    disc = disc.intersect(dome)
    return disc.faces("%SPHERE").edges().fillet(EYE_EDGE_R)


body = body.union(eye(+1)).union(eye(-1))

# ---------------- pin holes ----------------
hole = (
    cq.Workplane("YZ", origin=(-W / 2.0 - 5, 0, HOLE_Z))
    .circle(HOLE_D / 2.0)
    .extrude(W + 10)
)
body = body.cut(hole)

cbore = (
    cq.Workplane("YZ", origin=(W / 2.0 + EYE_BULGE - CB_DEPTH, 0, HOLE_Z))
    .circle(CB_D / 2.0)
    .extrude(CB_DEPTH + 5)
)
body = body.cut(cbore)

hex_pocket = (
    cq.Workplane("YZ", origin=(-W / 2.0 - 5, 0, HOLE_Z))
    .transformed(rotate=(0, 0, 90))
    .polygon(6, HEX_AF / math.cos(math.radians(30)))
    .extrude(HEX_DEPTH + 5 - EYE_BULGE)
)
body = body.cut(hex_pocket)

# ---------------- mounting plate ----------------
plate = (
    cq.Workplane(cq.Plane(origin=p_front, xDir=u, normal=n))
    .center(PLATE_LEN / 2.0, 0)
    .rect(PLATE_LEN, PLATE_H)
    .extrude(PLATE_T)
)

result = body.union(plate)

VIEW = {"azimuth": 45, "elevation": 26}
